import math
import cadquery as cq
from OCP.gp import gp_Ax2, gp_Pnt, gp_Dir, gp_Circ
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # base plate side length (square)
T = 6.0            # base plate thickness
H = 66.0           # overall height (base bottom to post tops)
HOLE_D = 80.0      # central round hole in base plate
LEG = 26.0         # leg length of the right-triangle corner posts

# lifting rings on top of the corner posts (vertical, parallel to the post diagonal face)
PR_OUT = 12.6      # outer radius of post ring
PR_TUBE = 2.55     # tube radius of post ring
PR_DROP = 0.0      # ring centre sits this far below the post top
PR_INSET = 2.0     # ring plane offset from the diagonal face toward the corner
# the ring on the (-X,+Y) post sits slightly off-centre along its face
PR_SHIFT = {(-1, 1): 0.7}

# lifting rings at the middle of the +/-Y base edges (horizontal)
BR_OUT = 9.0       # outer radius of base-edge ring
BR_TUBE = 2.0      # tube radius of base-edge ring
BR_Z = 3.98        # height of base ring centre above the plate bottom
BR_INSET = 0.0     # ring centre inset from the plate edge

VIEW = {"azimuth": 45, "elevation": 26}


def ring(R, r, center, axis, seam_dir, tube_seam_deg=180.0):
    """Torus (centre-line radius R, tube radius r) about `axis` through `center`.
    The profile seam is put on the `seam_dir` side (buried in the body); the
    tube seam sits at `tube_seam_deg` round the tube (0 = outer equator,
    90 = toward +axis, 180 = inner equator)."""
    c = cq.Vector(center)
    a = cq.Vector(axis).normalized()
    s = cq.Vector(seam_dir)
    s = (s - a * s.dot(a)).normalized()
    pc = c + s * R
    n = a.cross(s).normalized()
    ang = math.radians(tube_seam_deg)
    xd = s * math.cos(ang) + a * math.sin(ang)
    ax2 = gp_Ax2(gp_Pnt(pc.x, pc.y, pc.z), gp_Dir(n.x, n.y, n.z),
                 gp_Dir(xd.x, xd.y, xd.z))
    e = cq.Edge(BRepBuilderAPI_MakeEdge(gp_Circ(ax2, r)).Edge())
    w = cq.Wire.assembleEdges([e])
    return cq.Solid.revolve(w, [], 360, c, c + a)


# ---------------- base plate ----------------
plate = cq.Workplane("XY").box(W, W, T, centered=(True, True, False))
# through hole; cylinder seam turned toward the (+X,-Y) side where no view sees it
bore = (
    cq.Solid.makeCylinder(HOLE_D / 2.0, T + 2.0, cq.Vector(0, 0, -1.0), cq.Vector(0, 0, 1))
    .rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -45)
)
part = plate.cut(cq.Workplane("XY").add(bore))

# ---------------- triangular corner posts with top rings ----------------
h = W / 2.0
for sx in (1, -1):
    for sy in (1, -1):
        pts = [
            (sx * h, sy * h),
            (sx * (h - LEG), sy * h),
            (sx * h, sy * (h - LEG)),
        ]
        post = cq.Workplane("XY").polyline(pts).close().extrude(H)
        part = part.union(post)

        n = cq.Vector(sx, sy, 0).normalized()       # toward the corner
        mid = h - LEG / 2.0 + PR_INSET / math.sqrt(2.0)
        t = cq.Vector(-sy, sx, 0).normalized()       # along the diagonal face
        sh = PR_SHIFT.get((sx, sy), 0.0)
        c = cq.Vector(sx * mid, sy * mid, H - PR_DROP) + t * sh
        rg = ring(PR_OUT - PR_TUBE, PR_TUBE, c, n, t)
        part = part.union(cq.Workplane("XY").add(rg))

# ---------------- rings on the +/-Y base edges ----------------
for sy in (1, -1):
    c = (0, sy * (h - BR_INSET), BR_Z)
    rg = ring(BR_OUT - BR_TUBE, BR_TUBE, c, (0, 0, 1), (0, -sy, 0), 270.0)
    part = part.union(cq.Workplane("XY").add(rg))

result = part
